import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
U = 10.0                 # column pitch / comb plate thickness
BASE_L = 13 * U          # base length (X)
BASE_W = 3 * U           # base depth (Y)
BASE_T = 1 * U           # base thickness (Z)
PIECE_T = U              # comb plate thickness (Y)

# column heights above the base top, 5 columns per comb plate
# (column 2 is the narrow slot between the tall outer post and the stepped body)
HEIGHTS_A = [79.25, 10.0, 41.2, 67.25, 14.8]
HEIGHTS_B = [94.0, 17.8, 41.6, 82.5, 46.7]
PIECE_A_X0 = -5.5 * U    # left edge of comb plate A
PIECE_B_X0 = 0.5 * U     # left edge of comb plate B (gap of one pitch between plates)

EMBOSS_H = 1.8           # height of the small raised marks
LETTER_SIZE = 6.5        # font size of the raised A / B labels
LETTER_Y = -10.15        # Y position of the label centres (in front of the plates)
TRI_BASE = 4.0           # triangle mark base width (X)
TRI_HEIGHT = 4.0         # triangle mark height (Y)
CIRC_D = 3.0             # circle mark diameter

LABEL_TEXT = "data/pilot/Set35/id-02/Type3-Rep01"
LABEL_SIZE = 6.1         # font size of the engraved underside text
LABEL_DEPTH = 0.3        # engraving depth of the underside text


def comb_plate(x0, heights):
    """Stepped comb plate: one closed XZ profile extruded symmetric in Y."""
    pts = [(x0, BASE_T)]
    for i, h in enumerate(heights):
        pts.append((x0 + i * U, BASE_T + h))
        pts.append((x0 + (i + 1) * U, BASE_T + h))
    pts.append((x0 + len(heights) * U, BASE_T))
    return (
        cq.Workplane("XZ")
        .polyline(pts)
        .close()
        .extrude(PIECE_T / 2, both=True)
    )


# base plate
base = cq.Workplane("XY").box(BASE_L, BASE_W, BASE_T, centered=(True, True, False))

plate_a = comb_plate(PIECE_A_X0, HEIGHTS_A)
plate_b = comb_plate(PIECE_B_X0, HEIGHTS_B)

result = base.union(plate_a).union(plate_b)

# raised triangle mark centred on the floor of slot A
slot_a_cx = PIECE_A_X0 + 1.5 * U
slot_a_z = BASE_T + HEIGHTS_A[1]
tri = (
    cq.Workplane("XY", origin=(slot_a_cx, 0, slot_a_z))
    .polyline(
        [
            (-TRI_BASE / 2, -TRI_HEIGHT / 2),
            (TRI_BASE / 2, -TRI_HEIGHT / 2),
            (0, TRI_HEIGHT / 2),
        ]
    )
    .close()
    .extrude(EMBOSS_H)
)
result = result.union(tri)

# raised round mark centred on the floor of slot B
slot_b_cx = PIECE_B_X0 + 1.5 * U
slot_b_z = BASE_T + HEIGHTS_B[1]
circ = (
    cq.Workplane("XY", origin=(slot_b_cx, 0, slot_b_z))
    .circle(CIRC_D / 2)
    .extrude(EMBOSS_H)
)
result = result.union(circ)

# raised A / B labels on the base top, centred in front of each plate
for label, x0 in (("A", PIECE_A_X0), ("B", PIECE_B_X0)):
    cx = x0 + 2.5 * U
    try:
        txt = cq.Workplane("XY", origin=(cx, LETTER_Y, BASE_T)).text(
            label, LETTER_SIZE, EMBOSS_H, halign="center", valign="center"
        )
        result = result.union(txt)
    except Exception:
        pass

# shallow engraved identification text on the underside (reads from below)
try:
    under = cq.Workplane(
        cq.Plane(origin=(0, 0, LABEL_DEPTH), xDir=(1, 0, 0), normal=(0, 0, -1))
    ).text(LABEL_TEXT, LABEL_SIZE, LABEL_DEPTH, halign="center", valign="center")
    # kerned glyphs may overlap slightly: fuse them into one tool body first
    glyphs = under.val().Solids()
    tool = glyphs[0].fuse(*glyphs[1:]).clean() if len(glyphs) > 1 else glyphs[0]
    engraved = result.cut(cq.Workplane("XY").add(tool))
    if engraved.val().isValid():
        result = engraved
except Exception:
    pass

VIEW = {"azimuth": 45, "elevation": 26}
